import math
import cadquery as cq

# Snap-clip / latch lever: a constant-section profile (eye boss with bore,
# S-shaped spring arm, toothed finger, curved paddle body with side notch and
# heel) extruded along Z, with chamfered top and bottom outlines.

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------------------------------------------------------------------
# Driving dimensions (mm).  Profile lies in XY, extruded along +Z.
# ---------------------------------------------------------------------------
H = 29.6            # extrusion height
EYE_R = 8.2         # outer radius of the eye boss
HOLE_R = 4.25       # through hole in the eye
CHAMFER = 0.6       # top / bottom edge chamfer

# S-shaped arm: constant-width band around a lead-in / arc / line / arc / tail
# centreline; its two edges are smooth splines through the exact offsets
ARM_W = 6.6
C1 = (1.6, -14.0)   # upper bend centre
R1 = 9.3            # upper bend centreline radius
C2 = (4.85, -29.35) # lower bend centre
R2 = 5.0            # lower bend centreline radius
A_START = 45.0      # angle on the upper bend where the straight lead-in joins
LEAD_LEN = 6.0      # straight lead-in of the arm, starting inside the eye
EXIT_DIR = 228.5    # angle on lower bend where arm leaves heading down-right
TAIL_LEN = 19.0     # length of the straight tail running into the body

# Toothed finger
FX0, FX1 = 15.75, 21.5   # left / right face of finger
FY_TOP = -21.8           # top of finger
F_RTL, F_RTR = 2.0, 2.0  # top corner radii
N_TEETH = 5              # number of grooves on the finger's outer face
TOOTH_Y0 = -25.95        # centre of the first (top) groove
TOOTH_P = 3.1            # groove pitch
TOOTH_D = 1.2            # groove depth
GROOVE_W = 1.0           # groove width (round bottom, radius GROOVE_W / 2)
RIDGE_R = 0.7            # rounding of the ridge edges (<= TOOTH_D - GROOVE_W / 2)

# Big right-hand face: convex shoulder + two concave sweeps
RA = 10.0                 # shoulder radius
CB = (25.3, -61.76)       # first concave sweep centre
RB = 15.35
RC = 50.9                 # second (long) concave sweep radius
CC_DIR = (32.8, -14.24)   # direction from CB to the centre of the long sweep
Y_BOTTOM_CORNER = -89.9
# arc-length stations (fraction of the construction chain) used for the spline
RIGHT_FRACS = (0.09, 0.184, 0.27, 0.351, 0.6, 1.0)

# Notch on the left side of the lower body
NOTCH_C = (0.35, -59.14)
NOTCH_R = 4.46
TIP = (-8.06, -65.42)     # sharp tip of the left protrusion (before rounding)
TIP_DIR = (0.79, 0.615)   # direction of the protrusion's upper edge

# corner roundings (vertical edges)
R_TIP = 0.8
R_NOTCH_EDGE = 0.7
R_SHOULDER_L = 2.5
R_V = 1.2
R_BOTTOM = 1.5
R_HEEL = 1.0


# ---------------------------------------------------------------------------
# helpers
# ---------------------------------------------------------------------------
def pol(c, r, a_deg):
    a = math.radians(a_deg)
    return (c[0] + r * math.cos(a), c[1] + r * math.sin(a))


def ang(c, p):
    return math.degrees(math.atan2(p[1] - c[1], p[0] - c[0]))


def chord_params(pts):
    out = [0.0]
    for a, b in zip(pts[:-1], pts[1:]):
        out.append(out[-1] + math.hypot(b[0] - a[0], b[1] - a[1]))
    return out


def spline_to(wp, pts, t0=None, t1=None):
    """chord-length parametrised spline from the current point through pts"""
    cur = wp._findFromPoint(False)
    allp = [(cur.x, cur.y)] + list(pts)
    tans = None
    if t0 is not None and t1 is not None:
        tans = [t0, t1]
    return wp.spline(pts, tangents=tans, parameters=chord_params(allp), scale=False,
                     includeCurrent=True)


def arc_mid(c, r, a0, a1, ccw):
    """point half way along the arc from angle a0 to a1 (deg)"""
    if ccw:
        while a1 <= a0:
            a1 += 360.0
    else:
        while a1 >= a0:
            a1 -= 360.0
    return pol(c, r, (a0 + a1) / 2.0)


# ---------------------------------------------------------------------------
# Eye boss
# ---------------------------------------------------------------------------
eye = cq.Workplane("XY").circle(EYE_R).extrude(H)

# ---------------------------------------------------------------------------
# S arm : centreline (CW arc, tangent line, CCW arc, tangent line), offset
# ---------------------------------------------------------------------------
dx, dy = C2[0] - C1[0], C2[1] - C1[1]
L12 = math.hypot(dx, dy)
beta = math.degrees(math.acos((R1 + R2) / L12))
n_ang = math.degrees(math.atan2(dy, dx)) + beta          # normal at tangency
T1 = pol(C1, R1, n_ang)
T2 = pol(C2, R2, n_ang + 180.0)
P_arc0 = pol(C1, R1, A_START)
h0 = math.radians(A_START - 90.0)                        # CW tangent heading
P_start = (P_arc0[0] - LEAD_LEN * math.cos(h0), P_arc0[1] - LEAD_LEN * math.sin(h0))
P_mid1 = arc_mid(C1, R1, A_START, n_ang, False)
a2_0 = n_ang + 180.0
P_mid2 = arc_mid(C2, R2, a2_0, EXIT_DIR, True)
P_exit = pol(C2, R2, EXIT_DIR)
hd = math.radians(EXIT_DIR + 90.0)                       # CCW tangent heading
P_end = (P_exit[0] + TAIL_LEN * math.cos(hd), P_exit[1] + TAIL_LEN * math.sin(hd))

# centreline segments: lead-in line, CW arc, tangent line, CCW arc, tail line
arm_segs = [
    ("L", P_start, P_arc0),
    ("A", C1, R1, A_START, n_ang),
    ("L", T1, T2),
    ("A", C2, R2, a2_0, EXIT_DIR),
    ("L", P_exit, P_end),
]


def seg_length(s):
    if s[0] == "L":
        return math.hypot(s[2][0] - s[1][0], s[2][1] - s[1][1])
    return abs(math.radians(s[4] - s[3])) * s[2]


def seg_point(s, f, off):
    """point at fraction f of segment s, offset 'off' to the left of travel"""
    if s[0] == "L":
        dx_, dy_ = s[2][0] - s[1][0], s[2][1] - s[1][1]
        ln = math.hypot(dx_, dy_)
        nx, ny = -dy_ / ln, dx_ / ln
        return (s[1][0] + dx_ * f + off * nx, s[1][1] + dy_ * f + off * ny)
    c, r, a0, a1 = s[1], s[2], s[3], s[4]
    a = a0 + (a1 - a0) * f
    ccw = a1 > a0
    rr = r - off if ccw else r + off
    return pol(c, rr, a)


arm_len = [seg_length(s) for s in arm_segs]
arm_total = sum(arm_len)


def arm_point(frac, off):
    sl = arm_total * frac
    for s, ln in zip(arm_segs, arm_len):
        if sl <= ln + 1e-9:
            return seg_point(s, sl / ln, off)
        sl -= ln
    return seg_point(arm_segs[-1], 1.0, off)


# stations along the centreline (fractions of its length) for the edge splines
cum = [0.0]
for ln in arm_len:
    cum.append(cum[-1] + ln / arm_total)


def _between(a, b, n):
    return [a + (b - a) * k / (n + 1) for k in range(1, n + 1)]


# (lead-in, upper bend, straight, lower bend, tail) interior station counts
ARM_STATIONS = (1, 3, 0, 3, 2)
ARM_FRACS = [0.0]
for i_seg, n_st in enumerate(ARM_STATIONS):
    ARM_FRACS += _between(cum[i_seg], cum[i_seg + 1], n_st) + [cum[i_seg + 1]]

h_start = (P_arc0[0] - P_start[0], P_arc0[1] - P_start[1])
lh = math.hypot(*h_start)
h_start = (h_start[0] / lh, h_start[1] / lh)
h_end = (math.cos(hd), math.sin(hd))

left_pts = [arm_point(f, ARM_W / 2.0) for f in ARM_FRACS]
right_pts_arm = [arm_point(f, -ARM_W / 2.0) for f in ARM_FRACS]

arm = cq.Workplane("XY").moveTo(*right_pts_arm[0])
arm = spline_to(arm, right_pts_arm[1:], h_start, h_end)
arm = arm.lineTo(*left_pts[-1])
arm = spline_to(arm, left_pts[-2::-1], (-h_end[0], -h_end[1]), (-h_start[0], -h_start[1]))
arm = arm.close().extrude(H)

# ---------------------------------------------------------------------------
# Big right-hand face: construction chain of tangent arcs (convex shoulder off
# the finger, short concave sweep, long concave sweep) carried by one spline
# ---------------------------------------------------------------------------
# shoulder circle: centre (FX1-RA, yA), externally tangent to circle B
ddx = FX1 - RA - CB[0]
yA = CB[1] + math.sqrt((RA + RB) ** 2 - ddx ** 2)
CA = (FX1 - RA, yA)
k = RB / (RA + RB)
T_AB = (CB[0] + k * (CA[0] - CB[0]), CB[1] + k * (CA[1] - CB[1]))
lc = math.hypot(*CC_DIR)
u = (CC_DIR[0] / lc, CC_DIR[1] / lc)
CC = (CB[0] + (RC - RB) * u[0], CB[1] + (RC - RB) * u[1])
T_BC = (CB[0] - RB * u[0], CB[1] - RB * u[1])
P_BR = (CC[0] - math.sqrt(RC ** 2 - (Y_BOTTOM_CORNER - CC[1]) ** 2), Y_BOTTOM_CORNER)

aA0, aA1 = 0.0, ang(CA, T_AB)
P_Am = arc_mid(CA, RA, aA0, aA1, False)
aB0, aB1 = ang(CB, T_AB), ang(CB, T_BC)
P_Bm = arc_mid(CB, RB, aB0, aB1, True)
aC0, aC1 = ang(CC, T_BC), ang(CC, P_BR)
if aC1 < aC0:
    aC1 += 360.0
if aA1 > aA0:
    aA1 -= 360.0
if aB1 < aB0:
    aB1 += 360.0
# sample the tangent arc chain uniformly; a single spline is put through it
segs = [(CA, RA, aA0, aA1), (CB, RB, aB0, aB1), (CC, RC, aC0, aC1)]
seg_len = [abs(math.radians(s[3] - s[2])) * s[1] for s in segs]
tot_len = sum(seg_len)
right_pts = []
for fr in RIGHT_FRACS:
    sl = tot_len * fr
    for (c, r, a0, a1), ln in zip(segs, seg_len):
        if sl <= ln + 1e-9:
            right_pts.append(pol(c, r, a0 + (a1 - a0) * sl / ln))
            break
        sl -= ln
ta = math.radians(aC1 + 90.0)
t_end = (math.cos(ta), math.sin(ta))

# ---------------------------------------------------------------------------
# notch on the left side
# ---------------------------------------------------------------------------
px, py = TIP[0] - NOTCH_C[0], TIP[1] - NOTCH_C[1]
lu = math.hypot(*TIP_DIR)
ux, uy = TIP_DIR[0] / lu, TIP_DIR[1] / lu
bq = px * ux + py * uy
cq_ = px * px + py * py - NOTCH_R ** 2
tq = -bq - math.sqrt(bq * bq - cq_)
P_notch0 = (TIP[0] + tq * ux, TIP[1] + tq * uy)
a_n0 = ang(NOTCH_C, P_notch0)
a_n1 = 65.7
P_notch1 = pol(NOTCH_C, NOTCH_R, a_n1)
P_notchm = arc_mid(NOTCH_C, NOTCH_R, a_n0, a_n1, True)

HEEL_CORNER = (0.05, -83.2)
HEEL_PTS = [(5.5, -91.15), (2.0, -91.97), (-0.3, -90.66), (-1.56, -88.71),
            (-1.9, -86.43), (-1.27, -84.48)]
LEFT_PTS = [(-0.45, -80.5), (-1.1, -74.55), (-3.38, -70.02), (-6.0, -67.2)]
SHOULDER_PTS = [(4.7, -50.5), (7.2, -47.0), (8.0, -43.5), (8.4, -41.0)]

# ---------------------------------------------------------------------------
# toothed outer face of the finger: N_TEETH round-bottomed grooves whose
# mouths are rounded, so the ridges between them come out as rounded ribs
# each groove: convex round -> wall -> round bottom -> wall -> convex round
# ---------------------------------------------------------------------------
tooth_path = []          # sequence of ("line", end) / ("arc", mid, end)
rg = GROOVE_W / 2.0
for i in range(N_TEETH):
    yc = TOOTH_Y0 - i * TOOTH_P
    y_up, y_dn = yc + rg, yc - rg
    # convex round at the upper mouth, centre inside the ridge above
    c_up = (FX1 - RIDGE_R, y_up + RIDGE_R)
    tooth_path.append(("line", (FX1, y_up + RIDGE_R)))
    tooth_path.append(("arc", pol(c_up, RIDGE_R, -45.0), (FX1 - RIDGE_R, y_up)))
    # upper wall, round bottom, lower wall (walls vanish when the rounds meet)
    wall = (FX1 - RIDGE_R) - (FX1 - TOOTH_D + rg)
    if wall > 1e-6:
        tooth_path.append(("line", (FX1 - TOOTH_D + rg, y_up)))
    tooth_path.append(("arc", (FX1 - TOOTH_D, yc), (FX1 - TOOTH_D + rg, y_dn)))
    if wall > 1e-6:
        tooth_path.append(("line", (FX1 - RIDGE_R, y_dn)))
    # convex round at the lower mouth
    c_dn = (FX1 - RIDGE_R, y_dn - RIDGE_R)
    tooth_path.append(("arc", pol(c_dn, RIDGE_R, 45.0), (FX1, y_dn - RIDGE_R)))

# ---------------------------------------------------------------------------
# Finger + lower body outline (clockwise)
# ---------------------------------------------------------------------------
body = (
    cq.Workplane("XY")
    .moveTo(FX0, -44.0)
    .lineTo(FX0, FY_TOP - F_RTL)
    .threePointArc(pol((FX0 + F_RTL, FY_TOP - F_RTL), F_RTL, 135), (FX0 + F_RTL, FY_TOP))
    .lineTo(FX1 - F_RTR, FY_TOP)
    .threePointArc(pol((FX1 - F_RTR, FY_TOP - F_RTR), F_RTR, 45), (FX1, FY_TOP - F_RTR))
)
for seg in tooth_path:
    if seg[0] == "line":
        body = body.lineTo(*seg[1])
    else:
        body = body.threePointArc(seg[1], seg[2])
body = body.lineTo(FX1, yA)
# one smooth face through the shoulder / concave sweep construction
body = spline_to(body, right_pts, (0.0, -1.0), t_end)
# bottom end and rounded heel
body = spline_to(body, HEEL_PTS + [HEEL_CORNER])
# left edge up to the protrusion tip
body = spline_to(body, LEFT_PTS + [TIP])
body = body.lineTo(*P_notch0).threePointArc(P_notchm, P_notch1)
# shoulder running up into the S arm
body = spline_to(body, SHOULDER_PTS)
body = body.lineTo(11.0, -43.5).close()
body = body.extrude(H)

part = eye.union(arm).union(body)


# ---------------------------------------------------------------------------
# round selected vertical corner edges
# ---------------------------------------------------------------------------
def vertical_edges(wp):
    out = []
    for e in wp.edges().vals():
        a, b = e.startPoint(), e.endPoint()
        if abs(a.x - b.x) < 1e-4 and abs(a.y - b.y) < 1e-4 and abs(a.z - b.z) > 1e-3:
            out.append(e)
    return out


def round_edge(wp, xy, r):
    """fillet the vertical (Z-parallel) edge closest to plan position xy"""
    best = min(vertical_edges(wp), key=lambda e: math.hypot(e.Center().x - xy[0], e.Center().y - xy[1]))
    return wp.newObject([best]).fillet(r)


# location of the corner where the arm's outer edge runs into the body
corner_L = (8.0, -43.0)
corner_V = (FX0, -41.6)

part = round_edge(part, TIP, R_TIP)
part = round_edge(part, P_notch0, R_NOTCH_EDGE)
part = round_edge(part, P_notch1, R_NOTCH_EDGE)
part = round_edge(part, corner_L, R_SHOULDER_L)
part = round_edge(part, corner_V, R_V)
part = round_edge(part, P_BR, R_BOTTOM)
part = round_edge(part, HEEL_CORNER, R_HEEL)

# ---------------------------------------------------------------------------
# through hole
# ---------------------------------------------------------------------------
part = part.cut(cq.Workplane("XY").circle(HOLE_R).extrude(H))

# ---------------------------------------------------------------------------
# chamfer round the top and bottom outline (the bore stays sharp)
# ---------------------------------------------------------------------------
outer_edges = part.faces(">Z").val().outerWire().Edges() + part.faces("<Z").val().outerWire().Edges()
part = part.newObject(outer_edges).chamfer(CHAMFER)

result = part
